import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# X : along the arm, Y : plate thickness direction (wall side +Y), Z : up
# Boss axis is the Y axis (X=0, Z=0)
# ---------------------------------------------------------------
PLATE_T = 7.0            # arm plate thickness (Y)
ARM_BOT_Z = -6.7         # bottom edge of the arm
ARM_TOP_Z0 = 9.8         # top edge height at X = ARM_TOP_X0
ARM_TOP_X0 = 12.7
ARM_SLOPE = 0.263        # slope of the arm top edge
ARM_END_X = 201.8        # right end of the plate
EDGE_R = 3.0             # fillet of the plate outline edges
HOLE_EDGE_R = 3.4        # fillet around the lightening cut-outs

# boss (revolved about Y)
BOSS_FRONT_Y = -20.6
BOSS_FRONT_R = 11.4
BOSS_R = 13.1
BOSS_BACK_Y = 6.0
BOSS_CYL_Y = 3.5         # start of the short cylindrical end of the boss
BOSS_FRONT_FILLET = 1.8
BORE_D = 13.0            # main bore in the boss (from the front)
BORE_DEPTH = 17.0
BORE_FILLET = 0.6
BORE2_D = 9.0            # smaller continuation of the bore
BORE2_DEPTH = 25.0

# neck + wall flange
FLANGE_Y0 = 34.0
FLANGE_T = 2.0
FLANGE_R = 17.0
FLANGE_CH_FRONT = 0.9
FLANGE_CH_BACK = 0.4
NECK_HALF_H = 6.9        # flats of the neck (Z)
WIN_Y0, WIN_Y1 = 6.4, 32.2   # see-through window in the neck (Y range)
WIN_W0, WIN_W1, WIN_W2 = 7.0, 6.0, 7.9   # window half widths: boss end, middle, flange end

# clips
CLIP_X = 210.5
CLIP_RO = 10.0
CLIP_RI = 7.2
CLIP_STRAIGHT = 5.8      # straight part of the clip walls (+Y)
CLIP_H = 20.0
CLIP1_ZC = 0.4           # centre height of the lower clip
CLIP2_ZC = 54.0          # centre height of the upper clip
CLIP_LIP_R = 1.9        # bead radius on the lips
CLIP_LIP_OUT = 0.5      # outward flare of the lip beads
CLIP_EDGE_R = 1.2


def arm_top(x):
    return ARM_TOP_Z0 + ARM_SLOPE * (x - ARM_TOP_X0)


def rounded_poly(wp, pts, radii):
    """Closed polygon with tangent-arc rounded corners on workplane wp."""
    n = len(pts)
    data = []
    for i in range(n):
        P = pts[i]
        A = pts[i - 1]
        B = pts[(i + 1) % n]
        r = radii[i] if isinstance(radii, (list, tuple)) else radii
        u1 = (A[0] - P[0], A[1] - P[1])
        l1 = math.hypot(*u1)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (B[0] - P[0], B[1] - P[1])
        l2 = math.hypot(*u2)
        u2 = (u2[0] / l2, u2[1] / l2)
        cth = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        th = math.acos(cth)
        d = r / math.tan(th / 2.0)
        t1 = (P[0] + u1[0] * d, P[1] + u1[1] * d)
        t2 = (P[0] + u2[0] * d, P[1] + u2[1] * d)
        bx, by = u1[0] + u2[0], u1[1] + u2[1]
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        h = r / math.sin(th / 2.0)
        c = (P[0] + bx * h, P[1] + by * h)
        m = (c[0] - bx * r, c[1] - by * r)
        data.append((t1, m, t2))
    w = wp.moveTo(*data[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = data[i % n]
        w = w.lineTo(*t1).threePointArc(m, t2)
    return w.close()


# ---------------------------------------------------------------
# Arm plate (profile in XZ, extruded symmetric in Y)
# ---------------------------------------------------------------
plate_pts = [
    (0.0, ARM_BOT_Z),
    (ARM_END_X, ARM_BOT_Z),
    (ARM_END_X, arm_top(ARM_END_X)),
    (0.0, arm_top(0.0)),
]
plate = (
    cq.Workplane("XZ")
    .polyline(plate_pts).close()
    .extrude(PLATE_T / 2.0, both=True)
)
# round the outline edges of the plate on the visible (front, -Y) side only;
# the wall side (+Y) keeps sharp edges
plate = plate.faces("<Y").edges().fillet(EDGE_R)

# lightening cut-outs (truss)
TOP_OFF = 11.2
c1 = [(73.3, 4.3), (112.6, 4.3), (112.6, arm_top(112.6) - TOP_OFF),
      (73.3, arm_top(73.3) - TOP_OFF)]
c1_r = [4.8, 3.2, 3.2, 4.8]

c2 = [(119.6, 4.3), (142.6, 4.3), (142.6, 11.6), (119.6, 18.9)]
c2_r = [3.0, 3.5, 3.5, 3.0]


def diag_lower(x):
    return 21.4 - 0.238 * (x - 142.9)


# apex of the big triangular opening
xa = (21.4 + 0.238 * 142.9 - (ARM_TOP_Z0 - ARM_SLOPE * ARM_TOP_X0 - TOP_OFF)) / (ARM_SLOPE + 0.238)
c3 = [(xa, diag_lower(xa)), (192.8, diag_lower(192.8)), (192.8, arm_top(192.8) - TOP_OFF)]
c3_r = [5.8, 3.0, 3.0]

for pts, rr in ((c1, c1_r), (c2, c2_r), (c3, c3_r)):
    cutter = rounded_poly(cq.Workplane("XZ").workplane(offset=-10), pts, rr).extrude(20)
    plate = plate.cut(cutter)


def _inner_edge(e):
    c = e.Center()
    d = e.tangentAt(0.5)
    if abs(d.y) > 0.9:
        return False
    return (30.0 < c.x < ARM_END_X - 4.0 and c.z > ARM_BOT_Z + 4.0
            and c.z < arm_top(c.x) - 4.0)


plate = plate.newObject([e for e in plate.edges().vals() if _inner_edge(e)]).fillet(HOLE_EDGE_R)

# ---------------------------------------------------------------
# Boss (revolved about the Y axis)
# ---------------------------------------------------------------
boss = (
    cq.Workplane("XY")
    .moveTo(0.0, BOSS_FRONT_Y)
    .lineTo(BOSS_FRONT_R, BOSS_FRONT_Y)
    .spline([(BOSS_R - 1.05, BOSS_FRONT_Y + 7.3),
             (BOSS_R - 0.45, BOSS_FRONT_Y + 14.2),
             (BOSS_R - 0.08, BOSS_FRONT_Y + 20.1),
             (BOSS_R, BOSS_CYL_Y)],
            tangents=[(0.09, 1.0), (0.0, 1.0)],
            includeCurrent=True)
    .lineTo(BOSS_R, BOSS_BACK_Y)
    .lineTo(0.0, BOSS_BACK_Y)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), 90)      # put the revolve seam underneath
)
boss = boss.faces("<Y").edges().fillet(BOSS_FRONT_FILLET)

# ---------------------------------------------------------------
# Neck: revolved trumpet intersected with a Z-limited profile,
# with a see-through window along Z
# ---------------------------------------------------------------
neck_rev = (
    cq.Workplane("XY")
    .moveTo(0, BOSS_BACK_Y - 2)
    .lineTo(BOSS_R - 0.2, BOSS_BACK_Y - 2)
    .lineTo(BOSS_R - 0.2, BOSS_BACK_Y)
    .spline([(11.4, 10.0), (10.1, 19.0), (11.2, 27.0), (13.2, 31.0), (15.0, 33.0), (16.1, FLANGE_Y0 + 0.3)],
            includeCurrent=True)
    .lineTo(0, FLANGE_Y0 + 0.3)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), 90)
)

H = NECK_HALF_H
FY = FLANGE_Y0 + 0.3
# half-height of the neck (Z) along Y: fillet from the boss, slightly waisted
# middle (flats), then the flare into the wall flange
NECK_Z_PTS = [(8.1, 10.4), (10.4, H + 0.9), (13.7, H + 0.2), (19.0, H - 0.05), (24.0, H + 0.1),
              (26.8, H + 0.5), (29.2, 8.8), (30.7, 11.0), (32.1, 13.9), (33.2, 15.8), (FY, 16.6)]
neck_z = (
    cq.Workplane("YZ").workplane(offset=-30)
    .moveTo(BOSS_BACK_Y - 2, -20)
    .lineTo(BOSS_BACK_Y - 2, 20)
    .lineTo(BOSS_BACK_Y, 20)
    .lineTo(BOSS_BACK_Y, BOSS_R)
    .spline(NECK_Z_PTS, tangents=[(0.3, -1.0), (0.25, 1.0)], includeCurrent=True)
    .lineTo(FY, -16.6)
    .spline([(y, -z) for (y, z) in reversed(NECK_Z_PTS[:-1])] + [(BOSS_BACK_Y, -BOSS_R)],
            tangents=[(-0.25, 1.0), (-0.3, -1.0)], includeCurrent=True)
    .lineTo(BOSS_BACK_Y, -20)
    .close()
    .extrude(60)
)
neck = neck_rev.intersect(neck_z)

window = (
    cq.Workplane("XY").workplane(offset=-25)
    .moveTo(-WIN_W0, WIN_Y0)
    .lineTo(WIN_W0, WIN_Y0)
    .threePointArc((WIN_W1, 19.0), (WIN_W2, WIN_Y1))
    .lineTo(-WIN_W2, WIN_Y1)
    .threePointArc((-WIN_W1, 19.0), (-WIN_W0, WIN_Y0))
    .close()
    .extrude(50)
)
window = window.edges("|Z").fillet(2.2)
neck = neck.cut(window)

flange = (
    cq.Workplane("XZ").workplane(offset=-FLANGE_Y0)
    .circle(FLANGE_R).extrude(-FLANGE_T)
)
flange = flange.faces("<Y").edges().chamfer(FLANGE_CH_FRONT)
flange = flange.faces(">Y").edges().chamfer(FLANGE_CH_BACK)

# ---------------------------------------------------------------
# Clips (C-shaped, axis along Z, opening towards +Y)
# ---------------------------------------------------------------
def make_clip(zc):
    ro, ri, ys = CLIP_RO, CLIP_RI, CLIP_STRAIGHT
    rm = (ro + ri) / 2.0
    rb = CLIP_LIP_R
    x0 = CLIP_X
    z0 = zc - CLIP_H / 2.0
    off = rm + CLIP_LIP_OUT                      # bead centre distance from the clip axis
    dxo = ro - off
    dyo = math.sqrt(max(rb * rb - dxo * dxo, 0.0))
    dxi = off - ri
    dyi = math.sqrt(max(rb * rb - dxi * dxi, 0.0))
    w = (
        cq.Workplane("XY").workplane(offset=z0)
        .moveTo(x0 - ro, ys - dyo)
        .lineTo(x0 - ro, 0)
        .threePointArc((x0, -ro), (x0 + ro, 0))
        .lineTo(x0 + ro, ys - dyo)
        .threePointArc((x0 + off, ys + rb), (x0 + ri, ys - dyi))
        .lineTo(x0 + ri, 0)
        .threePointArc((x0, -ri), (x0 - ri, 0))
        .lineTo(x0 - ri, ys - dyi)
        .threePointArc((x0 - off, ys + rb), (x0 - ro, ys - dyo))
        .close()
        .extrude(CLIP_H)
    )
    w = w.faces("<Z or >Z").edges().fillet(CLIP_EDGE_R)
    return w


clip1 = make_clip(CLIP1_ZC)
clip2 = make_clip(CLIP2_ZC)

# ---------------------------------------------------------------
# Assemble
# ---------------------------------------------------------------
body = boss.union(neck).union(flange).union(plate).union(clip1).union(clip2)

# front bore (stepped) with a rounded entrance
bore = (
    cq.Workplane("XZ").workplane(offset=-BOSS_FRONT_Y)
    .circle(BORE_D / 2.0).extrude(-BORE_DEPTH)
)
bore2 = (
    cq.Workplane("XZ").workplane(offset=-BOSS_FRONT_Y)
    .circle(BORE2_D / 2.0).extrude(-BORE2_DEPTH)
)
body = body.cut(bore).cut(bore2)
body = body.faces("<Y").edges(cq.selectors.RadiusNthSelector(0)).fillet(BORE_FILLET)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
